import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# =====================================================================
#  Elbow cover / hood: a thin-walled arch-section hood that runs back
#  horizontally and then turns down at ~60 deg.  The front end carries a
#  reduced spigot (lip) with a curved rim, snap tongues and a latch slot.
#  X = width (symmetric), Y = front(-) -> back(+), Z = up.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 48.2          # half width of the hood at the front face (bottom of arch)
H = 60.0          # height of the front (horizontal) section at the front face
TAPER = 2.0       # draft of the hood, shrinking towards the back (deg)
LEG_ANG = 60.0    # leg inclination below horizontal (deg)
Y_KNEE = 11.0     # Y of the concave knee on the lower edge
LEG_H = 48.5      # perpendicular height of the leg (free edge -> crown top)
LEG_LEN = 72.0    # leg length measured along the free edge from the knee
R_CROWN = 75.0    # crown radius of the leg roof
R_BEND = 15.0     # blend radius between leg roof and hood arch (outer)
R_KNEE = 6.0      # concave fillet at the knee
R_TOE = 13.5      # rounded lower corner of the leg end
T = 1.5           # wall thickness
G = 4.5           # inset of the front spigot (lip) relative to the outer skin
LIP_R = 101.0     # radius of the curved front rim of the lip (axis along X)
LIP_CY, LIP_CZ = 80.3, 1.25   # centre of that rim radius
LIP_LEN = 25.0    # max forward extent used to build the lip
NOTCH_W = 23.5    # latch notch in the outer skin (along X)
NOTCH_Y0, NOTCH_Y1 = -0.5, 2.1   # notch extent along Y
NOTCH_Z = 50.0    # notch floor height
SLOT_W = 21.2     # latch slot through the lip top (along X)
SLOT_Y0, SLOT_Y1 = -4.35, 0.65
TAB_Z = [49.0, 31.5, 11.0]        # heights of the snap tongues on the rim
TAB_L, TAB_OUT, TAB_BUMP = 6.0, 1.5, 0.5   # tongue length, forward reach, hook bump

# ---------------- derived ----------------
a = math.radians(LEG_ANG)
D = cq.Vector(0, math.cos(a), -math.sin(a))      # leg direction (down/back)
N = cq.Vector(0, math.sin(a), math.cos(a))       # leg "up" direction
S_KNEE = Y_KNEE * math.cos(a)
U_FREE = Y_KNEE * math.sin(a)
U_ROOF = U_FREE + LEG_H
S_END = S_KNEE + LEG_LEN
Z_BOT = -90.0


def yz(s, u):
    p = D * s + N * u
    return (p.y, p.z)


# ---------------- hood arch profile (sketch x = X, sketch y = Z) ----------------
ARCH_PTS = [(0.0, H), (20.9, H - 3.2), (36.6, H - 15.0), (44.6, H - 31.8),
            (47.6, H - 50.0), (W, 0.0), (W, -30.0), (W, -60.0), (W, Z_BOT)]


def _base_edge():
    pts = [(-x, z) for (x, z) in reversed(ARCH_PTS[1:])] + ARCH_PTS
    vs = [cq.Vector(x, z, 0) for (x, z) in pts]
    return cq.Edge.makeSpline(vs, tangents=[cq.Vector(0, 1, 0), cq.Vector(0, -1, 0)]), pts


_BASE, _BASE_PTS = _base_edge()
_NS = 600
_SAMPLES = [_BASE.positionAt(i / float(_NS)) for i in range(_NS + 1)]


def _normal_at(p):
    # inward unit normal of the base arch near point p
    q = cq.Vector(p[0], p[1], 0)
    best = min(range(_NS + 1), key=lambda i: (_SAMPLES[i] - q).Length)
    i0, i1 = max(best - 1, 0), min(best + 1, _NS)
    t = (_SAMPLES[i1] - _SAMPLES[i0]).normalized()
    return (t.y, -t.x)


def arch_wire(off, zbot=Z_BOT):
    pts = []
    for p in _BASE_PTS:
        n = _normal_at(p)
        pts.append(cq.Vector(p[0] + n[0] * off, p[1] + n[1] * off, 0))
    pts[0] = cq.Vector(pts[0].x, zbot, 0)
    pts[-1] = cq.Vector(pts[-1].x, zbot, 0)
    sp = cq.Edge.makeSpline(pts, tangents=[cq.Vector(0, 1, 0), cq.Vector(0, -1, 0)])
    return cq.Wire.assembleEdges([sp, cq.Edge.makeLine(pts[-1], pts[0])])


def to_front_plane(w, y=0.0):
    # map sketch (x, z) to world (x, y, z)
    return w.moved(cq.Location(cq.Vector(0, y, 0), cq.Vector(1, 0, 0), 90))


def hood(offset, length=140.0):
    """drafted arch-section hood running back along +Y"""
    d = length * math.tan(math.radians(TAPER))
    w0 = to_front_plane(arch_wire(offset))
    w1 = to_front_plane(arch_wire(offset + d), length)
    return cq.Solid.makeLoft([w0, w1], True)


def prism(offset, y0, y1):
    """straight (undrafted) arch prism between y0 and y1"""
    w = to_front_plane(arch_wire(offset), y0)
    return cq.Solid.extrudeLinear(w, [], cq.Vector(0, y1 - y0, 0))


def crown(offset):
    """crowned roof of the inclined leg (cylinder along the leg axis)"""
    c = N * (U_ROOF - R_CROWN)
    return cq.Solid.makeCylinder(R_CROWN - offset, 400, c - D * 150, D)


def side_block():
    """side silhouette: front, floor, knee, inclined free edge, toe, end cut"""
    p_toe = yz(S_END, U_FREE)
    p_far = yz(S_END, U_ROOF + 40)
    pts = [(-10.0, 90.0), (-10.0, 0.0), (Y_KNEE, 0.0), p_toe, p_far, (p_far[0], 90.0)]
    wp = cq.Workplane("YZ").polyline(pts).close().extrude(80, both=True)
    wp = wp.edges("|X").edges(cq.selectors.NearestToPointSelector((0, Y_KNEE, 0))).fillet(R_KNEE)
    wp = wp.edges("|X").edges(cq.selectors.NearestToPointSelector((0, p_toe[0], p_toe[1]))).fillet(R_TOE)
    return wp.val()


def blend_edges(solid, r):
    """edges between the crown cylinder and the hood (not the end cut)"""
    out = []
    for f in solid.Faces():
        if f.geomType() != "CYLINDER":
            continue
        if abs(f._geomAdaptor().Cylinder().Radius() - r) > 1e-3:
            continue
        for e in f.Edges():
            if abs(e.Center().dot(D) - S_END) < 0.05:
                continue
            out.append(e)
    return out


# ---------------- outer skin and cavity ----------------
outer = side_block().intersect(hood(0.0)).intersect(crown(0.0))
outer = outer.fillet(R_BEND, blend_edges(outer, R_CROWN))

inner_box = cq.Solid.makeBox(200, 300, 300, cq.Vector(-100, T, -150))
inner = hood(T).intersect(crown(T)).intersect(inner_box)
inner = inner.fillet(R_BEND - T, blend_edges(inner, R_CROWN - T))

body = outer.cut(inner)

# ---------------- front spigot (lip) with curved rim ----------------
above_floor = cq.Solid.makeBox(200, 200, 200, cq.Vector(-100, -100, 0))
rim_cyl = cq.Solid.makeCylinder(LIP_R, 200, cq.Vector(-100, LIP_CY, LIP_CZ), cq.Vector(1, 0, 0))
lip_outer = prism(G, -LIP_LEN, T * 0.5).intersect(above_floor).intersect(rim_cyl)
lip_hole = prism(G + T, -LIP_LEN - 5, T + 2.0)
body = body.fuse(lip_outer).cut(lip_hole)


# ---------------- snap tongues on the lip rim ----------------
_LIP_SP = [e for e in arch_wire(G).Edges() if e.geomType() == "BSPLINE"][0]


def lip_point(zq):
    """point and outward normal on the +X half of the lip outer surface at height zq"""
    lo_, hi_ = 0.5, 0.95
    for _ in range(60):
        m = 0.5 * (lo_ + hi_)
        if _LIP_SP.positionAt(m).y > zq:
            lo_ = m
        else:
            hi_ = m
    p = _LIP_SP.positionAt(lo_)
    t = _LIP_SP.tangentAt(lo_)
    return p, cq.Vector(-t.y, t.x, 0).normalized()


def rim_y(zq):
    return LIP_CY - math.sqrt(LIP_R ** 2 - (zq - LIP_CZ) ** 2)


for zq in TAB_Z:
    p, n = lip_point(zq)
    ang = math.degrees(math.atan2(n.y, n.x))
    y_r = rim_y(zq)
    # local box: x = outward normal, y = along Y, z = along arch tangent
    tongue = cq.Solid.makeBox(T, TAB_OUT + 1.5, TAB_L, cq.Vector(-T, -TAB_OUT, -TAB_L / 2))
    bump = cq.Solid.makeBox(TAB_BUMP + 0.2, 1.0, TAB_L, cq.Vector(-0.2, -TAB_OUT, -TAB_L / 2))
    blk = tongue.fuse(bump)
    blk = blk.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 1, 0), -ang)
    blk = blk.translate(cq.Vector(p.x, y_r, p.y))
    body = body.fuse(blk).fuse(blk.mirror("YZ"))

# ---------------- latch: boss under the notch, notch and slot ----------------
boss = (cq.Workplane("XY").workplane(offset=NOTCH_Z - 1.5)
        .center(0, 2.6).slot2D(NOTCH_W + 4.0, 6.0).extrude(15).val())
boss = boss.intersect(hood(0.0)).intersect(cq.Solid.makeBox(60, 20, 30, cq.Vector(-30, SLOT_Y1, 40)))
body = body.fuse(boss)
notch = (cq.Workplane("XY").workplane(offset=NOTCH_Z)
         .center(0, 0.5 * (NOTCH_Y0 + NOTCH_Y1)).slot2D(NOTCH_W, NOTCH_Y1 - NOTCH_Y0).extrude(20).val())
body = body.cut(notch)
slot = (cq.Workplane("XY").workplane(offset=NOTCH_Z - 6)
        .center(0, 0.5 * (SLOT_Y0 + SLOT_Y1)).slot2D(SLOT_W, SLOT_Y1 - SLOT_Y0).extrude(20).val())
body = body.cut(slot)

result = cq.Workplane("XY").add(body)
